"""Open-top holder box with two angled screw lugs, a front tab and bottom windows.

Thin-walled rounded box (large back corner radii, small front ones), a
vertical slot in the middle of the front and back walls, two 45-degree lugs
at the front corners with a foot boss under each, a hollow cap tab on the
front wall and small windows at the foot of the side and back walls.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.0          # box outer width (X)
D = 35.5          # box outer depth (Y)
H = 47.0          # box height (Z)
T = 1.6           # wall thickness
TF = 1.1          # floor thickness
RB = 9.6          # back vertical corner radius (outer)
RF = 1.8          # front vertical corner radius (outer)
RF_IN = 0.6       # front vertical corner radius (inner)
RIM = 0.4         # rim rounding on the top edges
SLOT_FIL = 0.7    # rounding of the slot edges
BOT_FIL = 0.5     # rounding of the bottom outline

SLOT_W = 5.0      # central slot width (front and back walls)
SLOT_Z = 8.9      # bottom of slot (lowest point)

# ears (mounting lugs), 45 degrees outward from the front corners
EAR_DX = 4.5      # hole centre outboard of side wall
EAR_DY = 10.4     # hole centre in front of front wall
EAR_R = 8.6       # lug end radius
HOLE_D = 5.1      # lug hole diameter
EAR_Z0 = 6.4      # underside of lug plate
EAR_Z1 = 15.0     # top of lug plate
EAR_LEN = 30.0    # centre distance used for the lug arm (runs into the box)
EAR_FIL = 0.6     # lug edge rounding
HOLE_FIL = 0.3    # lug hole edge rounding
JOIN_FIL = 0.8    # lug top face to box wall blend

# foot boss under each lug (circle, centre given inboard / behind the front corner)
BOSS_CS = 7.42
BOSS_CV = 7.43
BOSS_R = 12.75

# tab on front wall (hollow cap, open underneath)
TAB_X0 = 8.4
TAB_X1 = 20.4
TAB_P = 8.2       # protrusion from front wall
TAB_Z0 = 5.6
TAB_Z1 = 18.8
TAB_R = 4.2       # top-front rounding
TAB_T = 1.2       # cap wall thickness

# bottom windows
WIN_Z0 = TF
WIN_Z1 = 5.4
WIN_R = 0.5
SIDE_WIN_Y0 = -10.65
SIDE_WIN_Y1 = 7.4
BACK_WIN_X0 = 14.9
BACK_WIN_X1 = 30.1


def rounded_box(w, d, h, rb, rf, z0=0.0):
    b = cq.Workplane("XY").box(w, d, h, centered=(True, True, False))
    b = b.edges("|Z and >Y").fillet(rb)
    if rf > 0.05:
        b = b.edges("|Z and <Y").fillet(rf)
    return b.translate((0, 0, z0))


def try_fillet(wp, edges, r):
    """Fillet the given edges, keeping the original if OCC cannot do it cleanly."""
    if not edges:
        return wp
    try:
        res = wp.newObject(edges).fillet(r)
        if res.val().isValid():
            return res
    except Exception:
        pass
    return wp


# ---------------- outer shell ----------------
outer = rounded_box(W, D, H, RB, RF)
outer = outer.faces("<Z").edges().fillet(BOT_FIL)

# ---------------- lugs ----------------
for sx in (-1, 1):
    hx = sx * (W / 2 + EAR_DX)
    hy = -D / 2 - EAR_DY
    ang = math.degrees(math.atan2(1.0, -sx))          # hole -> box direction
    ux, uy = -sx / math.sqrt(2), 1 / math.sqrt(2)
    cx, cy = hx + ux * EAR_LEN / 2, hy + uy * EAR_LEN / 2

    # lug plate: a slot shape running from the hole into the box
    arm = (
        cq.Workplane("XY")
        .workplane(offset=EAR_Z0)
        .center(cx, cy)
        .slot2D(EAR_LEN + 2 * EAR_R, 2 * EAR_R, ang)
        .extrude(EAR_Z1 - EAR_Z0)
    )
    arm = arm.faces(">Z").edges().fillet(EAR_FIL)
    arm = arm.faces("<Z").edges().fillet(EAR_FIL)
    hole = (
        cq.Workplane("XY")
        .workplane(offset=EAR_Z0 - 1)
        .center(hx, hy)
        .circle(HOLE_D / 2)
        .extrude(EAR_Z1 - EAR_Z0 + 2)
    )
    arm = arm.cut(hole)
    arm = arm.faces(">Z").edges(cq.selectors.RadiusNthSelector(0)).fillet(HOLE_FIL)

    # foot boss: a circle (centred just inside the box corner) clipped to the lug strip,
    # so its flat side continues the lug's outer face down to the floor
    bcx = sx * (W / 2 - BOSS_CS)
    bcy = -D / 2 + BOSS_CV
    bh = EAR_Z0 + 1.0                                   # overlaps the plate
    circ = cq.Workplane("XY").center(bcx, bcy).circle(BOSS_R).extrude(bh)
    strip = (
        cq.Workplane("XY")
        .center(cx, cy)
        .rect(EAR_LEN + 40, 2 * EAR_R)
        .extrude(bh)
        .rotate((cx, cy, 0), (cx, cy, 1), ang)
    )
    boss = circ.intersect(strip)
    boss = boss.faces("<Z").edges().fillet(BOT_FIL)
    outer = outer.union(boss).union(arm)


# ---------------- blend lug tops into the box walls ----------------
def on_box_outline(x, y, tol=0.02):
    """True if (x, y) lies on the outer rounded-rectangle outline of the box."""
    r = RB if y >= 0 else RF
    cx, cy = W / 2 - r, D / 2 - r
    ax, ay = abs(x), abs(y)
    if ax <= cx:
        return abs(ay - D / 2) < tol
    if ay <= cy:
        return abs(ax - W / 2) < tol
    return abs(math.hypot(ax - cx, ay - cy) - r) < tol


def junction_edges(wp, z):
    sel = []
    for e in wp.edges().vals():
        pts = [e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0)]
        if all(abs(p.z - z) < 1e-3 for p in pts) and all(on_box_outline(p.x, p.y) for p in pts):
            sel.append(e)
    return sel


outer = try_fillet(outer, junction_edges(outer, EAR_Z1), JOIN_FIL)

# ---------------- tab (hollow cap) ----------------
tab = (
    cq.Workplane("XY")
    .box(TAB_X1 - TAB_X0, TAB_P + T / 2, TAB_Z1 - TAB_Z0, centered=False)
    .translate((TAB_X0, -D / 2 - TAB_P, TAB_Z0))
)
tab = tab.edges("|X and >Z and <Y").fillet(TAB_R)
tab = tab.edges("|Z and <Y").fillet(0.6)
tab_in = (
    cq.Workplane("XY")
    .box(TAB_X1 - TAB_X0 - 2 * TAB_T, TAB_P - TAB_T + T / 2, TAB_Z1 - TAB_Z0 - TAB_T + 1,
         centered=False)
    .translate((TAB_X0 + TAB_T, -D / 2 - TAB_P + TAB_T, TAB_Z0 - 1))
)
tab_in = tab_in.edges("|X and >Z and <Y").fillet(TAB_R - TAB_T)
tab_in = tab_in.cut(cq.Workplane("XY").box(W, D, 3 * H))   # keep the hollow outside the wall
outer = outer.union(tab)

# ---------------- cavity ----------------
cavity = rounded_box(W - 2 * T, D - 2 * T, H, RB - T, RF_IN, z0=TF)
body = outer.cut(cavity).cut(tab_in)

# ---------------- slots in front and back walls ----------------
slot_cut = (
    cq.Workplane("XZ")
    .workplane(offset=-D)
    .center(0, (SLOT_Z + H + 5) / 2)
    .slot2D(H + 5 - SLOT_Z, SLOT_W, 90)
    .extrude(2 * D)
)
body = body.cut(slot_cut)

# ---------------- rim rounding (top edges and slot edges) ----------------
def slot_edges(wp):
    sel = []
    for e in wp.edges().vals():
        bb = e.BoundingBox()
        if (bb.zmin < H - 0.01 and max(abs(bb.xmin), abs(bb.xmax)) < SLOT_W / 2 + 0.01
                and bb.zmin > SLOT_Z - 0.01 and min(abs(bb.ymin), abs(bb.ymax)) > D / 2 - T - 0.01):
            sel.append(e)
    return sel


def top_edges(wp):
    return [e for e in wp.edges().vals() if e.BoundingBox().zmin > H - 0.01]


step1 = try_fillet(body, slot_edges(body), SLOT_FIL)
step2 = try_fillet(step1, top_edges(step1), RIM)
if step1 is body or step2 is step1:
    # fall back to one common radius for the rim and the slot edges
    step2 = try_fillet(body, slot_edges(body) + top_edges(body), RIM)
body = step2

# ---------------- windows at the foot of the walls ----------------
side_win = (
    cq.Workplane("XY")
    .box(W + 2, SIDE_WIN_Y1 - SIDE_WIN_Y0, WIN_Z1 - WIN_Z0, centered=(True, False, False))
    .translate((0, SIDE_WIN_Y0, WIN_Z0))
    .edges("|X")
    .fillet(WIN_R)
)
body = body.cut(side_win)
for sx in (-1, 1):
    x0, x1 = sorted((sx * BACK_WIN_X0, sx * BACK_WIN_X1))
    bw = (
        cq.Workplane("XY")
        .box(x1 - x0, 2 * T + 2, WIN_Z1 - WIN_Z0, centered=False)
        .translate((x0, D / 2 - T - 1, WIN_Z0))
        .edges("|Y")
        .fillet(WIN_R)
    )
    body = body.cut(bw)

result = body
